"""Sheet-metal L bracket with a hex weld-nut boss.

Coordinates (mm): X to the right, Y backwards (depth), Z up.
Origin: leg outer face (X=0) / flange top (Z=0) / front face (Y=0).
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
T = 2.9            # sheet thickness of the L bracket
D = 11.4           # bracket depth (Y)
FLANGE_X = -18.9   # flange free end X
R_BEND = 0.6       # outer radius of the main 90 deg bend

LEG_Z_BEND = -17.5 # Z of the small bend of the leg (mid-surface, virtual sharp)
LEG_ANG = 15.0     # small bend angle of the leg tip (deg, toward -X)
LEG_TIP = 4.1      # length of the bent leg tip (mid-surface, from virtual sharp)
LEG_RI = 0.0       # inner radius of the small leg bend (0 = sharp)

DH = 5.78          # hex boss depth (Y), boss is flush with the bracket front face
HEX_AF = 18.5      # hex across flats (pointy top)
HEX_XC = 5.2       # hex centre X (lower hex vertices sit on the flange top)
R_HEXFIL = 2.05    # fillet hex left face / flange top
R_LEGFIL = 3.85    # fillet hex lower-right face (extended) / leg outer face
BACK_CH = 0.65     # chamfer on the back edges of the hex boss
THREAD_D = 7.3     # threaded hole, modelled as a plain bore (between minor and major dia)

HOLE_D = 2.7       # small holes
FH1_X = -14.94     # flange hole 1 X (holes on the bracket mid depth)
FH2_X = -6.37      # flange hole 2 X
LH_S = 2.45        # leg hole position along the bent tip from the virtual bend

GUS_T = 2.32       # weld gusset behind the hex: height of its 45deg top face at the hex
GUS_R = 2.10       # weld gusset: width of its 45deg right face at the hex
GUS_XL = -3.47     # weld gusset: X of its 45deg left face at the hex back face
GUS_Z0 = -6.2      # weld gusset: bottom Z at the hex back face
GUS_K = 0.5        # weld gusset: bottom slope dZ/dY

CUT_Y0 = 5.13      # relief cut under the boss extension: point Y
CUT_Z0 = -6.72     # relief cut under the boss extension: point Z
CUT_K = 1.87       # relief cut slope dZ/dY

BEAD_Y = 5.5       # stiffening bead under the flange: centre Y
BEAD_W = 3.0       # bead width at the flange surface
BEAD_WB = 2.0      # bead width at its crest
BEAD_H = 0.35      # bead height

# ---------------- derived values ----------------
HEX_R = HEX_AF / math.sqrt(3.0)
HEX_ZC = HEX_R / 2.0          # lower hex vertices on the flange top (Z=0)
XL = HEX_XC - HEX_AF / 2.0    # hex left face
XR = HEX_XC + HEX_AF / 2.0    # hex right face
T30 = math.tan(math.radians(30))
Z_EXT = HEX_ZC - HEX_R - HEX_XC * T30   # lower-right hex face extended to X=0
HT = T / 2.0


def half_space(origin, normal, size=80.0):
    """Big box lying on the +normal side of the plane through origin."""
    pl = cq.Plane(origin=origin, normal=normal)
    return cq.Workplane(pl).rect(size, size).extrude(size)


# ---------------- leg outline with the small bend near the tip ----------------
a = math.radians(LEG_ANG)
tdir = (-math.sin(a), -math.cos(a))            # tip direction
tnrm = (math.cos(a), -math.sin(a))             # tip outward normal (+X side)
if LEG_RI > 0:
    tb = (LEG_RI + HT) * math.tan(a / 2.0)     # tangent length
    zt = LEG_Z_BEND + tb                       # start of the bend arc
    C = (-T - LEG_RI, zt)                      # bend centre (inner side = -X)

    def arc_pt(rad, ang):
        return (C[0] + rad * math.cos(ang), C[1] - rad * math.sin(ang))

    in_s, in_m, in_e = arc_pt(LEG_RI, 0), arc_pt(LEG_RI, a / 2), arc_pt(LEG_RI, a)
    out_s, out_m, out_e = (arc_pt(LEG_RI + T, 0), arc_pt(LEG_RI + T, a / 2),
                           arc_pt(LEG_RI + T, a))
else:
    # sharp bend: kinks on the bisector (mitre)
    mm = HT / math.cos(a / 2.0)
    bx, bz = math.cos(a / 2.0), -math.sin(a / 2.0)
    out_s = out_e = (-HT + mm * bx, LEG_Z_BEND + mm * bz)
    in_s = in_e = (-HT - mm * bx, LEG_Z_BEND - mm * bz)
    in_m = out_m = None
tipc = (-HT + LEG_TIP * tdir[0], LEG_Z_BEND + LEG_TIP * tdir[1])
tip_out = (tipc[0] + HT * tnrm[0], tipc[1] + HT * tnrm[1])
tip_in = (tipc[0] - HT * tnrm[0], tipc[1] - HT * tnrm[1])
z_leg_low = min(out_s[1], in_s[1])


def bracket_profile():
    """L bracket (flange + leg with bent tip) in the XZ plane."""
    w = (cq.Workplane("XZ")
         .moveTo(FLANGE_X, 0)
         .lineTo(-R_BEND, 0)
         .radiusArc((0, -R_BEND), R_BEND)
         .lineTo(*out_s))
    if LEG_RI > 0:
        w = w.threePointArc(out_m, out_e)
    w = w.lineTo(*tip_out).lineTo(*tip_in).lineTo(*in_e)
    if LEG_RI > 0:
        w = w.threePointArc(in_m, in_s)
    return w.lineTo(-T, -T).lineTo(FLANGE_X, -T).close()


def boss_profile():
    """Front plate outline: hex + weld extension down to the leg, with fillets
    (also overlaps the flange/leg so that the union is seamless)."""
    p_l1 = (XL, R_HEXFIL)
    p_l2 = (XL - R_HEXFIL, 0)
    tl = R_LEGFIL * T30
    p_r1 = (0, Z_EXT - tl)
    p_r2 = (tl * math.cos(math.radians(30)), Z_EXT + tl * math.sin(math.radians(30)))
    return (cq.Workplane("XZ")
            .moveTo(HEX_XC, HEX_ZC + HEX_R)
            .lineTo(XL, HEX_ZC + HEX_R / 2.0)
            .lineTo(*p_l1)
            .radiusArc(p_l2, R_HEXFIL)
            .lineTo(FLANGE_X + 1.0, 0)
            .lineTo(FLANGE_X + 1.0, -T)
            .lineTo(-T, -T)
            .lineTo(-T, z_leg_low)
            .lineTo(0, z_leg_low)
            .lineTo(*p_r1)
            .radiusArc(p_r2, R_LEGFIL)
            .lineTo(XR, HEX_ZC - HEX_R / 2.0)
            .lineTo(XR, HEX_ZC + HEX_R / 2.0)
            .close())


# Workplane("XZ") normal is -Y, so a negative extrude goes toward +Y (backwards)
bracket = bracket_profile().extrude(-D)

boss = boss_profile().extrude(-DH)
boss = boss.faces(">Y").edges().chamfer(BACK_CH)      # back edges of the hex boss

# relief cut at the back/bottom of the boss extension (plane with normal in YZ)
ya, yb = -2.0, D + 2.0
relief = (cq.Workplane("YZ")
          .polyline([(ya, CUT_Z0 + CUT_K * (ya - CUT_Y0)),
                     (yb, CUT_Z0 + CUT_K * (yb - CUT_Y0)),
                     (yb, -40.0), (ya, -40.0)]).close()
          .extrude(30.0)
          .translate((-5.0, 0, 0)))
boss = boss.cut(relief)

# the 45deg left plane of the weld gusset also trims the back-left-bottom corner of the boss
trimL = (half_space((GUS_XL, DH, 0), (-1, 1, 0))
         .intersect(half_space((0, DH, GUS_T), (0, -1, -1))))
boss = boss.cut(trimL)

body = bracket.union(boss)

# ---------------- weld gusset behind the hex, around the main bend ----------------
gusset = (half_space((0, DH - 0.3, 0), (0, 1, 0))                       # behind the hex
          .intersect(half_space((GUS_XL, DH, 0), (1, -1, 0)))            # 45deg left face
          .intersect(half_space((GUS_R, DH, 0), (-1, -1, 0)))            # 45deg right face
          .intersect(half_space((0, DH, GUS_T), (0, -1, -1)))            # 45deg top face
          .intersect(half_space((0, DH, GUS_Z0), (0, -GUS_K, 1))))       # sloped bottom
outside_L = (cq.Workplane("XZ")
             .polyline([(-10.0, -0.05), (-0.05, -0.05), (-0.05, -20.0),
                        (10.0, -20.0), (10.0, 10.0), (-10.0, 10.0)])
             .close()
             .extrude(-30.0).translate((0, -5.0, 0)))
body = body.union(gusset.intersect(outside_L))

# ---------------- shallow stiffening bead under the flange (along X) ----------------
bead = (cq.Workplane("YZ")
        .polyline([(BEAD_Y - BEAD_W / 2.0, -T + 0.05), (BEAD_Y + BEAD_W / 2.0, -T + 0.05),
                   (BEAD_Y + BEAD_WB / 2.0, -T - BEAD_H), (BEAD_Y - BEAD_WB / 2.0, -T - BEAD_H)])
        .close()
        .extrude(-T - FLANGE_X + 0.02)
        .translate((FLANGE_X, 0, 0)))
body = body.union(bead)

# ---------------- holes ----------------
# threaded hole of the hex boss (plain bore, along Y)
thread = (cq.Workplane("XZ").center(HEX_XC, HEX_ZC)
          .circle(THREAD_D / 2.0).extrude(-(DH + 1.0)).translate((0, -0.5, 0)))
body = body.cut(thread)

# two holes in the flange (along Z)
fholes = (cq.Workplane("XY").pushPoints([(FH1_X, D / 2.0), (FH2_X, D / 2.0)])
          .circle(HOLE_D / 2.0).extrude(10.0).translate((0, 0, -6.0)))
body = body.cut(fholes)

# hole in the bent leg tip (perpendicular to the tip)
hc = (-HT + LH_S * tdir[0], LEG_Z_BEND + LH_S * tdir[1])
lh_plane = cq.Plane(origin=(hc[0] - 3.0 * tnrm[0], D / 2.0, hc[1] - 3.0 * tnrm[1]),
                    xDir=(0, 1, 0), normal=(tnrm[0], 0, tnrm[1]))
body = body.cut(cq.Workplane(lh_plane).circle(HOLE_D / 2.0).extrude(6.0))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
